import math

import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 50.0          # plate width  (X)
L = 72.0          # plate length (Y)
T = 1.0           # plate thickness
R_FRONT = 4.0     # corner radius at -Y end
R_BACK = 0.3      # corner radius at +Y end
EDGE_R = 0.4      # rounding of the plate's lower edge

HOLE_FRONT_D = 2.5
HOLE_BACK_D = 2.8
HOLE_X = 21.3
HOLE_FRONT_Y = -32.5
HOLE_BACK_Y = 20.7
CSK_D = 3.9       # countersink diameter on the underside of every hole

H_STD = 2.6       # common height of clips / blocks
SOFT_R = 0.3      # soft rounding of moulded edges
SLAB_H = 2.65
CLIP_H = 2.85     # spring clip fins / blades / lugs
SIDE_H = 3.05
SIDE_EDGE_R = 0.95
TALL_H = 3.8
FENCE_H = 0.8
FENCE_T = 0.45
POCKET_D = 0.45   # depth of the ESP32 module pocket
TEXT_D = 0.2      # engraving depth of the label
TEXT_SIZE = 3.0


def prism(pts, h, z0=T):
    return cq.Workplane("XY").workplane(offset=z0).polyline(pts).close().extrude(h)


def box(x0, x1, y0, y1, h, z0=T):
    return (cq.Workplane("XY").workplane(offset=z0)
            .center((x0 + x1) / 2.0, (y0 + y1) / 2.0)
            .rect(abs(x1 - x0), abs(y1 - y0)).extrude(h))


def vfillet(wp, r):
    try:
        return wp.edges("|Z").fillet(r)
    except Exception:
        return wp


def rounded_hull(circles, h, z0=T):
    """Extrude the convex hull of corner circles (x, y, r), given counter-clockwise; r = 0 gives a sharp corner."""
    n = len(circles)
    tang = []
    for i in range(n):
        x1, y1, r1 = circles[i]
        x2, y2, r2 = circles[(i + 1) % n]
        dx, dy = x2 - x1, y2 - y1
        ln = math.hypot(dx, dy)
        ux, uy = dx / ln, dy / ln
        mx, my = uy, -ux
        phi = math.asin((r1 - r2) / ln)
        nx = math.cos(phi) * mx + math.sin(phi) * ux
        ny = math.cos(phi) * my + math.sin(phi) * uy
        tang.append(((x1 + r1 * nx, y1 + r1 * ny), (x2 + r2 * nx, y2 + r2 * ny), (nx, ny)))
    wp = cq.Workplane("XY").workplane(offset=z0).moveTo(*tang[-1][1])
    for i in range(n):
        x, y, r = circles[i]
        if r > 1e-9:
            n1, n2 = tang[i - 1][2], tang[i][2]
            bx, by = n1[0] + n2[0], n1[1] + n2[1]
            bl = math.hypot(bx, by)
            wp = wp.threePointArc((x + r * bx / bl, y + r * by / bl), tang[i][0])
        if i < n - 1:
            wp = wp.lineTo(*tang[i][1])
    return wp.close().extrude(h)


def topfillet(wp, r):
    try:
        return wp.faces(">Z").edges().fillet(r)
    except Exception:
        return wp


# ---------------- base plate ----------------
plate = cq.Workplane("XY").rect(W, L).extrude(T)
plate = plate.edges("|Z and <Y").fillet(R_FRONT)
plate = plate.edges("|Z and >Y").fillet(R_BACK)
try:
    plate = plate.faces("<Z").edges().fillet(EDGE_R)
except Exception:
    pass

parts = []

# ---------------- central slab with V notch ----------------
slab_pts = [(-15.45, -12.8), (15.35, -12.8), (15.35, -2.0), (3.25, -10.2),
            (-3.5, -10.2), (-15.45, -2.0)]
parts.append(topfillet(prism(slab_pts, SLAB_H), SOFT_R))


# ---------------- side connector blocks ----------------
SB_X0, SB_X1 = 18.6, 24.5          # inner / outer face
SB_Y0, SB_Y1 = -0.75, 14.1         # ends at the base
SB_BUMPS = (1.1, 5.6, 8.3, 12.9)   # small rounded bumps on top


def side_block(sign):
    h = SIDE_H
    wp = cq.Workplane("YZ", origin=(SB_X0, 0, T))
    prof = (wp.moveTo(SB_Y0, 0).lineTo(SB_Y0 + 0.9, h - 1.15)
            .threePointArc((SB_Y0 + 1.35, h - 0.3), (SB_Y0 + 2.05, h))
            .lineTo(SB_Y1 - 1.6, h)
            .threePointArc((SB_Y1 - 0.8, h - 0.3), (SB_Y1 - 0.45, h - 1.05))
            .lineTo(SB_Y1, 0).close())
    b0 = prof.extrude(SB_X1 - SB_X0)
    b = b0
    sel = [e for e in b0.edges().vals()
           if (abs(e.Center().x - SB_X0) < 1e-3 or abs(e.Center().x - SB_X1) < 1e-3)
           and e.Center().z > T + 0.3]
    for r in (SIDE_EDGE_R, 1.0, 0.8, 0.6):
        try:
            b = b0.newObject(sel).fillet(r)
            break
        except Exception:
            b = b0
    res = b
    for i, yc in enumerate(SB_BUMPS):
        z0 = T + h - 0.15 if 0 < i < len(SB_BUMPS) - 1 else T + h - 1.2
        bh = 1.0 if 0 < i < len(SB_BUMPS) - 1 else 2.05
        bump = box(20.8, 22.6, yc - 0.48, yc + 0.48, bh, z0=z0)
        try:
            bump = bump.faces(">Z").edges("|X").fillet(0.25)
        except Exception:
            pass
        res = res.union(bump)
    if sign < 0:
        res = res.mirror("YZ")
    return res


parts.append(side_block(1))
parts.append(side_block(-1))

# ---------------- boss with recess ----------------
BOSS_X, BOSS_Y, BOSS_D, BOSS_HOLE = 12.5, 17.0, 4.7, 2.3
BOSS_RECESS = 0.5
boss = (cq.Workplane("XY").workplane(offset=T).center(BOSS_X, BOSS_Y)
        .circle(BOSS_D / 2.0).extrude(H_STD))
parts.append(boss)

# ---------------- top-left block A, pin, block B, top-right wedge ----------------
blockA = [(-15.4, 35.0), (-11.0, 35.0), (-10.2, 31.7), (-13.05, 27.2),
          (-13.25, 25.0), (-15.4, 24.85)]
parts.append(topfillet(vfillet(prism(blockA, H_STD), 0.8), SOFT_R))

blockB = [(-15.4, 20.7), (-12.3, 20.7), (-14.05, 17.8), (-12.6, 14.7), (-15.4, 13.3)]
parts.append(topfillet(vfillet(prism(blockB, H_STD), 0.5), SOFT_R))

pin = (cq.Workplane("XY").workplane(offset=T).center(-9.85, 25.3)
       .transformed(rotate=(0, 0, -66.0))
       .slot2D(4.9, 1.15).extrude(H_STD))
pin = topfillet(pin, 0.2)
parts.append(pin)

wedge = [(11.3, 35.0), (15.35, 35.0), (15.35, 27.95), (9.45, 32.8)]
parts.append(topfillet(prism(wedge, H_STD), SOFT_R))


# ---------------- spring clips (mirrored pair) ----------------
def vfillet_at(wp, spec):
    """fillet vertical edges located near the given (x, y) points with their own radius"""
    for (x, y), r in spec:
        try:
            sel = [e for e in wp.edges("|Z").vals()
                   if abs(e.Center().x - x) < 0.05 and abs(e.Center().y - y) < 0.05]
            if sel:
                wp = wp.newObject(sel).fillet(r)
        except Exception:
            pass
    return wp


def clip_left():
    t = 0.45
    top = (-12.9, 8.3)
    bend = (-13.3, 1.9)
    end = (-6.85, -3.1)
    fin_pts = [(top[0] - t, top[1]), (top[0] + t, top[1]),
               (bend[0] + t + 0.35, bend[1] + 0.6), (end[0] + 0.3, end[1] + 0.45),
               (end[0] - 0.3, end[1] - 0.45), (bend[0] - t, bend[1] - 0.4)]
    fin = prism(fin_pts, CLIP_H)
    fin = vfillet_at(fin, [(fin_pts[0], 0.4), (fin_pts[1], 0.4), (fin_pts[5], 1.0), (fin_pts[2], 0.3)])
    fin = topfillet(fin, 0.15)
    # tapered blade with a rounded tip at the end of the diagonal arm
    blade = rounded_hull([(-6.40, -2.76, 0.0), (-7.20, -3.84, 0.0), (-2.38, -6.50, 0.32)], CLIP_H)
    blade = topfillet(blade, 0.25)
    # rounded triangular lug
    tri = rounded_hull([(-7.67, 3.25, 0.9), (-9.865, 9.185, 0.5), (-10.44, 4.49, 0.5)], CLIP_H)
    tri = topfillet(tri, 0.25)
    return fin.union(blade).union(tri)


cl = clip_left()
parts.append(cl)
parts.append(cl.mirror("YZ"))

# ---------------- tall component near the -Y/+X corner ----------------
tall = vfillet(box(13.7, 17.0, -31.1, -19.2, TALL_H), 1.0)
try:
    tall = tall.faces(">Z").edges().fillet(0.35)
except Exception:
    pass
parts.append(tall)
parts.append(box(14.5, 16.2, -26.4, -23.8, 1.25, z0=T + TALL_H - 0.1))
for yc in (-20.3, -30.0):
    parts.append(box(14.3, 16.4, yc - 0.25, yc + 0.25, 1.2, z0=T + TALL_H - 0.1))

# ---------------- three push buttons at the front ----------------
for xc in (-0.76, 5.63, 12.06):
    btn = box(xc - 1.2, xc + 1.2, -31.8, -29.6, 2.0)
    try:
        btn = btn.faces(">Z").edges("<Y").chamfer(0.6)
    except Exception:
        pass
    parts.append(btn)
    parts.append(box(xc - 1.2, xc + 1.2, -33.2, -31.7, 1.15))

# ---------------- fence along the front end ----------------
FX_OUT, FX_IN, FY_TOP, FY_JOG, FY_FRONT = 22.3, 19.6, -18.8, -30.2, -33.4
fence_path = [(-FX_OUT, FY_TOP), (-FX_OUT, FY_JOG), (-FX_IN, FY_JOG), (-FX_IN, FY_FRONT),
              (FX_IN, FY_FRONT), (FX_IN, FY_JOG), (FX_OUT, FY_JOG), (FX_OUT, FY_TOP)]
for (a, b) in zip(fence_path[:-1], fence_path[1:]):
    x0, x1 = sorted([a[0], b[0]])
    y0, y1 = sorted([a[1], b[1]])
    parts.append(box(x0 - FENCE_T / 2, x1 + FENCE_T / 2, y0 - FENCE_T / 2, y1 + FENCE_T / 2, FENCE_H))

# ---------------- small SMD pads ----------------
for sx in (-1, 1):
    for yc in (-3.3, -13.4, -19.6, -25.5):
        # "I0" shaped two-part SMD pads: thin bar on the outside + small cube
        parts.append(box(sx * 20.4, sx * 21.65, yc - 0.65, yc + 0.65, 1.15))
        parts.append(box(sx * 21.9, sx * 22.5, yc - 0.75, yc + 0.75, 1.05))
parts.append(box(7.6, 9.3, -25.7, -24.75, 1.2))
parts.append(box(7.6, 9.3, -24.35, -23.4, 1.2))
parts.append(box(17.3, 18.4, -30.9, -29.5, 0.9))

# ---------------- ESP32 module pocket: corner wedges and castellation tabs ----------------
PAD_X0, PAD_X1, PAD_Y0, PAD_Y1 = -14.3, -2.8, -30.4, -21.5
ZF = T - POCKET_D   # pocket floor
tabs = [box(x0, x1, -21.95, -20.05, 1.0 + POCKET_D, z0=ZF) for (x0, x1) in [(-8.45, -6.95), (-4.25, -2.8)]]
tabs.append(box(-15.3, -14.1, -24.7, -23.0, 1.0 + POCKET_D, z0=ZF))

# ---------------- assemble ----------------
body = plate
for p in parts:
    body = body.union(p)

# mounting holes
for (hx, hy, d) in [(-HOLE_X, HOLE_FRONT_Y, HOLE_FRONT_D), (HOLE_X, HOLE_FRONT_Y, HOLE_FRONT_D),
                    (-HOLE_X, HOLE_BACK_Y, HOLE_BACK_D), (HOLE_X, HOLE_BACK_Y, HOLE_BACK_D)]:
    body = body.cut(cq.Workplane("XY").workplane(offset=-2).center(hx, hy).circle(d / 2.0).extrude(10))
    csk = cq.Solid.makeCone(CSK_D / 2.0 + 0.3, 0.0, CSK_D / 2.0 + 0.3,
                            pnt=cq.Vector(hx, hy, -0.3), dir=cq.Vector(0, 0, 1))
    body = body.cut(cq.Workplane("XY").add(csk))

# recess in the boss
body = body.cut(cq.Workplane("XY").workplane(offset=T + H_STD - BOSS_RECESS).center(BOSS_X, BOSS_Y)
                .circle(BOSS_HOLE / 2.0).extrude(5))

# module pocket with engraved label, then the wedges / tabs that stand in it
body = body.cut(box(PAD_X0, PAD_X1, PAD_Y0, PAD_Y1, 5.0, z0=ZF))
try:
    for (txt, xc, yc) in [("ESP32", -8.5, -23.9), ("ZERO", -8.4, -27.4)]:
        lab = (cq.Workplane("XY").workplane(offset=ZF - TEXT_D).center(xc, yc)
               .text(txt, TEXT_SIZE, TEXT_D + 0.5, kind="bold", halign="center", valign="center"))
        body = body.cut(lab)
except Exception:
    pass
for tb in tabs:
    body = body.union(tb)
body = body.union(prism([(-14.7, -28.0), (-11.5, -30.45), (-14.7, -30.45)], 1.3 + POCKET_D, z0=ZF))
body = body.union(prism([(-2.45, -28.0), (-2.45, -30.45), (-5.7, -30.45)], 1.3 + POCKET_D, z0=ZF))

result = body
